import cadquery as cq
from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
from OCP.Geom import Geom_TrimmedCurve
from OCP.BRep import BRep_Tool
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

# Bumper style phone case standing upright: width X, height Z, thickness Y.
# The open (phone) side faces -Y, the back with the embossed logo faces +Y.

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 63.0        # width  (X)
H = 128.0       # height (Z)
T = 12.85       # thickness (Y) without the back emboss
CORNER_L = 12.4 # length of the curvature-continuous corner blend (front view)
CORNER_D = 3.0  # inset of the corner blend on the diagonal
BACK_CH = 4.1   # chamfer on the back outer edge
BACK_R = 3.4    # fillet blending that chamfer into the back face
FRONT_CH = 0.85 # small chamfer on the front outer edge
WALL = 1.9      # side wall thickness
FLOOR_Y = -T / 2 + 9.16  # y of the cavity floor (inner face of the back plate)
C_IN_X, C_IN_Y = 1.4, 1.4    # chamfer at the cavity floor (in-plane, depth)

# side (-X) button openings
BTN_Y = -2.3
MUTE_Z, MUTE_W, MUTE_H = 44.2, 3.0, 6.0
VOL_Z = (32.6, 22.3)
VOL_D = 5.3
BTN_C = 0.5          # 45 deg chamfer on the outer edge of the side openings

# top power slot
PWR_X, PWR_Y = 13.2, -1.55
PWR_L, PWR_W = 10.7, 2.8
PWR_C = 0.7

# bottom slot
BOT_X, BOT_Y = 1.6, -2.6
BOT_L, BOT_W = 39.2, 5.6

# inner square mark
SQ_X, SQ_Z, SQ_W, SQ_H, SQ_D = -17.0, 2.0, 5.6, 4.9, 0.3

# embossed lettering and sail logo on the back face (letters read downwards seen from the back)
EMB = 0.35                # emboss height
FONT_SIZE = 18.4          # cap height ~13.4 mm
TXT1, TXT1_X, TXT1_Z = "POCARI", -18.2, (36.0, 20.8, 4.2, -9.2, -26.4, -39.8)
TXT2, TXT2_X, TXT2_Z = "SWEAT", -4.2, (35.9, 16.0, -0.4, -13.8, -29.9)
SAIL_TIP = (7.0, 38.1)
SAIL_LEFT = [(8.6, 32.4), (10.1, 25.3), (13.35, 15.85), (16.5, 6.4), (19.2, -2.8), (20.7, -11.7),
             (21.6, -20.2), (22.0, -28.7), (21.7, -41.2)]
SAIL_RIGHT = [(7.7, -41.0), (9.7, -19.7), (8.95, -5.2), (7.85, 7.1), (6.36, 19.4), (5.9, 31.5)]

# small rectangular notch on the -X side at the back edge
NOTCH_Y, NOTCH_Z, NOTCH_W, NOTCH_H, NOTCH_D = T / 2 - BACK_CH + 0.5, 2.5, 2.0, 5.2, 0.8


def _join(edges):
    """Concatenate tangent-continuous edges into one B-spline edge."""
    conv = None
    for e in edges:
        f, l = e._bounds()
        tc = Geom_TrimmedCurve(BRep_Tool.Curve_s(e.wrapped, 0.0, 1.0), f, l)
        if conv is None:
            conv = GeomConvert_CompCurveToBSplineCurve(tc)
        else:
            conv.Add(tc, 1e-7)
    return cq.Edge(BRepBuilderAPI_MakeEdge(conv.BSplineCurve()).Edge())


def outline(w, h, L, d, split=True):
    """Closed rounded-rectangle outline in the XZ plane (y=0).
    Corners are curvature-continuous quintic Bezier blends of length L and diagonal inset d.
    split=True : 4 smooth edges (top cap, right side, bottom cap, left side; the caps contain
                 the corner blends) -> faces with compact bounding boxes near the back emboss.
    split=False: a single smooth closed edge (seam at the middle of the bottom edge)."""
    a = 0.387 * L
    b = (16 * L - 5 * a - 32 * d) / 10.0
    hw, hh = w / 2.0, h / 2.0
    V = cq.Vector

    def corner(cx, cz, d1x, d1z, d2x, d2z):
        P = [V(cx + d1x * L, 0, cz + d1z * L), V(cx + d1x * (L - a), 0, cz + d1z * (L - a)),
             V(cx + d1x * (L - b), 0, cz + d1z * (L - b)), V(cx + d2x * (L - b), 0, cz + d2z * (L - b)),
             V(cx + d2x * (L - a), 0, cz + d2z * (L - a)), V(cx + d2x * L, 0, cz + d2z * L)]
        return cq.Edge.makeBezier(P), P[0], P[5]

    tl, tl0, tl1 = corner(-hw, hh, 0, -1, 1, 0)
    tr, tr0, tr1 = corner(hw, hh, -1, 0, 0, -1)
    br, br0, br1 = corner(hw, -hh, 0, 1, -1, 0)
    bl, bl0, bl1 = corner(-hw, -hh, 1, 0, 0, 1)
    if not split:
        # one single smooth edge, seam at the middle of the bottom edge
        m = V(0, 0, -hh)
        e = _join([cq.Edge.makeBezier([m, bl0]), bl, cq.Edge.makeBezier([bl1, tl0]), tl,
                   cq.Edge.makeBezier([tl1, tr0]), tr, cq.Edge.makeBezier([tr1, br0]), br,
                   cq.Edge.makeBezier([br1, m])])
        return cq.Wire.assembleEdges([e])
    top = _join([tl, cq.Edge.makeBezier([tl1, tr0]), tr])
    bottom = _join([br, cq.Edge.makeBezier([br1, bl0]), bl])
    right = cq.Edge.makeLine(tr1, br0)
    left = cq.Edge.makeLine(bl1, tl0)
    return cq.Wire.assembleEdges([top, right, bottom, left])


def inset(off, split=False):
    """Outline offset inwards by 'off' (corner blend kept concentric)."""
    return outline(W - 2 * off, H - 2 * off, CORNER_L - off, CORNER_D - 0.2929 * off, split)


def at(wire, y):
    return wire.translate(cq.Vector(0, y, 0))


# ---------------- body ----------------
# straight side band with a small front chamfer (one seamless ruled loft of the outline) ...
band = cq.Solid.makeLoft([at(inset(FRONT_CH), -T / 2), at(inset(0), -T / 2 + FRONT_CH),
                          at(inset(0), T / 2 - BACK_CH)], True)
# ... and the large back chamfer (split outline so the back faces stay compact)
back = cq.Solid.makeLoft([at(inset(0, True), T / 2 - BACK_CH), at(inset(BACK_CH, True), T / 2)], True)
body = cq.Workplane("XY").add(band).union(cq.Workplane("XY").add(back), glue=True)
body = body.faces(">Y").edges().fillet(BACK_R)          # roll the back chamfer into the back face

# cavity (open towards -Y) with a chamfered floor edge
cav = cq.Workplane("XY").add(
    cq.Solid.extrudeLinear(at(inset(WALL), -T / 2 - 2.0), [], cq.Vector(0, FLOOR_Y - C_IN_Y + T / 2 + 2.0, 0)))
floor_ch = cq.Solid.makeLoft([at(inset(WALL), FLOOR_Y - C_IN_Y), at(inset(WALL + C_IN_X), FLOOR_Y)], True)
cav = cav.union(cq.Workplane("XY").add(floor_ch))
body = body.cut(cav)

# side openings on the -X wall (mute switch slot + two volume holes), chamfered outside
xw = -W / 2


def rrect_x(x, w, h, r):
    """Closed rounded-rectangle wire in the plane x = const, centred on the mute switch."""
    c = cq.Vector(x, BTN_Y, MUTE_Z)
    pts = [c + cq.Vector(0, sy * w / 2, sz * h / 2) for sy, sz in ((-1, -1), (1, -1), (1, 1), (-1, 1))]
    poly = cq.Wire.makePolygon(pts, close=True)
    return poly.fillet2D(r, poly.Vertices())


def rrect_prism(x0, x1, w, h, r):
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(rrect_x(x0, w, h, r), [], cq.Vector(x1 - x0, 0, 0)))


mute = rrect_prism(xw - 1, xw + WALL + 2, MUTE_W, MUTE_H, 1.0)
mute_ch = cq.Workplane("XY").add(cq.Solid.makeLoft([
    rrect_x(xw - 0.01, MUTE_W + 2 * BTN_C + 0.02, MUTE_H + 2 * BTN_C + 0.02, 1.0 + BTN_C),
    rrect_x(xw + BTN_C, MUTE_W, MUTE_H, 1.0)], True))
body = body.cut(mute).cut(mute_ch)
for z in VOL_Z:
    vol = (cq.Workplane("YZ").workplane(offset=xw - 1)
           .center(BTN_Y, z).circle(VOL_D / 2).extrude(WALL + 3))
    vol_ch = cq.Solid.makeCone(VOL_D / 2 + BTN_C + 0.01, VOL_D / 2, BTN_C + 0.01,
                               cq.Vector(xw - 0.01, BTN_Y, z), cq.Vector(1, 0, 0))
    body = body.cut(vol).cut(cq.Workplane("XY").add(vol_ch))

# power slot through the top wall, chamfered rim
pwr = (cq.Workplane("XY").workplane(offset=H / 2 - WALL - 1)
       .center(PWR_X, PWR_Y).slot2D(PWR_L, PWR_W).extrude(WALL + 3))
pwr_ch = (cq.Workplane("XY").workplane(offset=H / 2 - PWR_C)
          .center(PWR_X, PWR_Y).slot2D(PWR_L, PWR_W)
          .workplane(offset=PWR_C + 0.01).slot2D(PWR_L + 2 * PWR_C + 0.02, PWR_W + 2 * PWR_C + 0.02)
          .loft(ruled=True))
body = body.cut(pwr).cut(pwr_ch)

# long slot through the bottom wall
bot = (cq.Workplane("XY").workplane(offset=-H / 2 - 1)
       .center(BOT_X, BOT_Y).slot2D(BOT_L, BOT_W).extrude(WALL + 3))
body = body.cut(bot)

# shallow square mark on the inner back face
sq = (cq.Workplane("XY").box(SQ_W, 2 * SQ_D, SQ_H)
      .edges("|Y").fillet(0.5)
      .translate((SQ_X, FLOOR_Y, SQ_Z)))
body = body.cut(sq)

# notch on the -X side at the back edge
notch = cq.Workplane("XY").box(2 * NOTCH_D, NOTCH_W, NOTCH_H).translate((-W / 2, NOTCH_Y, NOTCH_Z))
body = body.cut(notch)

# ---------------- back face emboss ----------------
yb = T / 2


def letter(ch, xc, zc):
    pl = cq.Plane(origin=(0, yb - 0.05, 0), xDir=(0, 0, -1), normal=(0, 1, 0))
    t = cq.Workplane(pl).text(ch, FONT_SIZE, EMB + 0.05, font="DejaVu Sans", kind="regular",
                              halign="center", valign="center")
    bb = t.val().BoundingBox()
    return t.translate((xc - bb.center.x, 0, zc - bb.center.z))


try:
    emb = None
    for txt, xc, zs in ((TXT1, TXT1_X, TXT1_Z), (TXT2, TXT2_X, TXT2_Z)):
        for ch, zc in zip(txt, zs):
            l = letter(ch, xc, zc)
            emb = l if emb is None else emb.union(l)
    body = body.union(emb)
except Exception:
    pass

# sail shaped logo
sail = (cq.Workplane("XZ", origin=(0, yb - 0.05, 0))
        .moveTo(*SAIL_TIP)
        .spline(SAIL_LEFT, includeCurrent=True)
        .lineTo(*SAIL_RIGHT[0])
        .spline(SAIL_RIGHT[1:] + [SAIL_TIP], includeCurrent=True)
        .close()
        .extrude(-(EMB + 0.05)))
body = body.union(sail)

result = body
